import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length (X)
W = 39.0           # overall width (Y)
T_TOP = 3.6        # thickness of the top cap plate
T_LIP = 1.9        # height of the stepped lip under the cap
LIP_INSET = 0.95   # lip inset from cap outline
RIM = 0.9          # lip wall thickness
POCKET = T_LIP     # depth of the underside recess (floor = cap underside)
R_LEFT = 4.2       # plan corner radius (hole end)
R_RIGHT = 2.2      # plan corner radius (clip end)
TOP_FILLET = 2.0   # rounding of the top cap edge
HOLE_X = -24.2     # threaded hole position
HOLE_Y = -0.3
HOLE_D = 8.0       # threaded hole (threads omitted)
BOSS_D = 9.6       # rounded boss around the hole on the underside
BOSS_H = 0.6
GRID_X = -L / 2 + 0.85 * L   # 3x3 grid of square light holes (centre)
GRID_Y = -W / 2 + 8.1
GRID_P = 4.6
SQ = 1.9

CLIP_LEN = 11.2    # snap clip length along X (centred under the grid)
CLIP_T = 1.3       # hook leg thickness
CLIP_DROP = 4.1    # hook reach below the lip
CLIP_REC = 0.12                        # front hook face sits just behind the lip face
CLIP_Y0 = -W / 2 + LIP_INSET + CLIP_REC  # outer face of front hook
CLIP_CLR = 0.0                         # lip notch clearance at the hook ends
CLIP_GAP = 11.7                        # distance between hook legs (inner faces)
FOOT = 0.9
FOOT_H = 1.0

RELIEF = 0.8       # depth of the engraved lettering
WAVE_DEPTH = 0.9   # depth of the round-bottomed wifi grooves
DOT_DEPTH = 1.0    # depth of the spherical wifi dimple
WIFI_DOT_C = (7.6, -1.5)
WIFI_DOT_D = 6.3
WIFI_ARC_C = (7.8, -1.2)
WIFI_W = 2.7
WIFI_ARCS = [(8.2, -3.0, 130.0), (13.8, 6.0, 121.0)]   # (radius, start deg, end deg)
CENTER_DOT = (0.2, -0.9)
CENTER_DOT_D = 1.6
TXT_SIZE = 8.3
# "DUST" over the hole, "SENSOR" under it (x, y, baseline angle)
LETTERS = [
    ("D", -32.2, 6.9, 40.0), ("U", -25.8, 11.1, 10.0), ("S", -18.1, 10.4, -27.0), ("T", -12.8, 6.1, -50.0),
    ("S", -35.2, -3.8, -68.0), ("E", -32.5, -9.8, -41.0), ("N", -25.5, -12.3, -7.0),
    ("S", -18.5, -12.3, 14.0), ("O", -12.4, -10.3, 19.0), ("R", -4.5, -7.5, 20.0),
]

Z_LIP = T_LIP
Z_TOP = T_LIP + T_TOP


def plan(l, w, rl, rr):
    """rounded rectangle with different radii at the two ends"""
    x0, x1 = -l / 2, l / 2
    y0, y1 = -w / 2, w / 2
    k = 0.70710678
    s = (cq.Workplane("XY")
         .moveTo(x0 + rl, y0)
         .lineTo(x1 - rr, y0)
         .threePointArc((x1 - rr + rr * k, y0 + rr - rr * k), (x1, y0 + rr))
         .lineTo(x1, y1 - rr)
         .threePointArc((x1 - rr + rr * k, y1 - rr + rr * k), (x1 - rr, y1))
         .lineTo(x0 + rl, y1)
         .threePointArc((x0 + rl - rl * k, y1 - rl + rl * k), (x0, y1 - rl))
         .lineTo(x0, y0 + rl)
         .threePointArc((x0 + rl - rl * k, y0 + rl - rl * k), (x0 + rl, y0))
         .close())
    return s


# ---------------- main body ----------------
cap = plan(L, W, R_LEFT, R_RIGHT).extrude(T_TOP).translate((0, 0, Z_LIP))
cap = cap.faces(">Z").edges().fillet(TOP_FILLET)

lip = plan(L - 2 * LIP_INSET, W - 2 * LIP_INSET,
           R_LEFT - LIP_INSET, R_RIGHT - LIP_INSET).extrude(Z_LIP + 0.01)
body = cap.union(lip)

# underside recess
ins = LIP_INSET + RIM
pocket = plan(L - 2 * ins, W - 2 * ins, R_LEFT - ins, R_RIGHT - ins).extrude(POCKET)
body = body.cut(pocket)

# boss around the threaded hole
boss = (cq.Workplane("XY").workplane(offset=POCKET - BOSS_H)
        .center(HOLE_X, HOLE_Y).circle(BOSS_D / 2).extrude(BOSS_H + 0.05))
boss = boss.faces("<Z").edges().fillet(BOSS_H * 0.8)
body = body.union(boss)
hole = cq.Workplane("XY").center(HOLE_X, HOLE_Y).circle(HOLE_D / 2).extrude(Z_TOP + 1).translate((0, 0, -1))
body = body.cut(hole)

# 3x3 square light holes through the cap
pts = [(GRID_X + i * GRID_P, GRID_Y + j * GRID_P) for i in (-1, 0, 1) for j in (-1, 0, 1)]
sq = cq.Workplane("XY").pushPoints(pts).rect(SQ, SQ).extrude(Z_TOP + 1)
body = body.cut(sq)


# ---------------- snap clip: two hooked legs facing each other ----------------
def rounded_profile(wp, pts, radii):
    """closed polygon (axis-aligned corners) with per-corner fillet radii"""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        q, r_ = pts[i - 1], pts[(i + 1) % n]
        rad = radii[i]
        if rad <= 0:
            segs.append((p, None, p))
            continue
        d1 = (q[0] - p[0], q[1] - p[1])
        d2 = (r_[0] - p[0], r_[1] - p[1])
        l1 = math.hypot(*d1)
        l2 = math.hypot(*d2)
        u1 = (d1[0] / l1, d1[1] / l1)
        u2 = (d2[0] / l2, d2[1] / l2)
        t1 = (p[0] + u1[0] * rad, p[1] + u1[1] * rad)
        t2 = (p[0] + u2[0] * rad, p[1] + u2[1] * rad)
        c = (p[0] + (u1[0] + u2[0]) * rad, p[1] + (u1[1] + u2[1]) * rad)
        b = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*b)
        m = (c[0] - b[0] / lb * rad, c[1] - b[1] / lb * rad)
        segs.append((t1, m, t2))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    return w.close()


def hook(y_outer, d):
    """d = +1: foot points +Y, d = -1: foot points -Y"""
    z_top, z_bot, z_ft = Z_LIP + 0.2, -CLIP_DROP, -CLIP_DROP + FOOT_H
    pts = [(y_outer, z_top), (y_outer + d * CLIP_T, z_top),
           (y_outer + d * CLIP_T, z_ft), (y_outer + d * (CLIP_T + FOOT), z_ft),
           (y_outer + d * (CLIP_T + FOOT), z_bot), (y_outer, z_bot)]
    radii = [0, 0, 0.3, 0.35, 0.35, 0.7]
    if d < 0:   # keep a consistent winding
        pts = pts[::-1]
        radii = radii[::-1]
    prof = rounded_profile(cq.Workplane("YZ"), pts, radii)
    return prof.extrude(CLIP_LEN / 2, both=True).translate((GRID_X, 0, 0))


# notch in the front lip where the front hook passes
notch = (cq.Workplane("XY").center(GRID_X, -W / 2 + LIP_INSET / 2 + RIM / 2)
         .rect(CLIP_LEN + 2 * CLIP_CLR, LIP_INSET + RIM + 0.4).extrude(Z_LIP))
body = body.cut(notch)
h1 = hook(CLIP_Y0, +1)
h2 = hook(CLIP_Y0 + 2 * CLIP_T + CLIP_GAP, -1)
body = body.union(h1).union(h2)


# ---------------- underside markings (engraved into the recess floor) ----------------
Z_ENG = POCKET - 0.05               # engraving tools start just below the floor
ENG_H = RELIEF + 0.05


def ball_groove(cx, cy, r, a0, a1):
    """round-bottomed groove along a circular arc with ball ends (wifi wave)"""
    rt = WIFI_W / 2                              # tool radius
    zc = POCKET + WAVE_DEPTH - rt                # tool centre height
    sweep = a1 - a0
    # revolve the tool section about the global Z axis through the arc centre
    ring = (cq.Workplane("XY").add(
        cq.Solid.revolve(cq.Face.makeFromWires(
            cq.Wire.makeCircle(rt, cq.Vector(r, 0, zc), cq.Vector(0, 1, 0))),
            sweep, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))))
    g = ring
    for a in (0.0, sweep):
        ar = math.radians(a)
        g = g.union(cq.Workplane("XY").add(
            cq.Solid.makeSphere(rt * 1.03, cq.Vector(r * math.cos(ar), r * math.sin(ar), zc))))
    return g.rotate((0, 0, 0), (0, 0, 1), a0).translate((cx, cy, 0))


def dimple(cx, cy, d, depth):
    """spherical dimple of given rim diameter and depth"""
    a = d / 2
    rs = (a * a + depth * depth) / (2 * depth)
    return cq.Workplane("XY").add(
        cq.Solid.makeSphere(rs, cq.Vector(cx, cy, POCKET + depth - rs)))


# engraving tools: wifi symbol (dimple + two round-bottomed waves), centre mark, lettering
marks = dimple(WIFI_DOT_C[0], WIFI_DOT_C[1], WIFI_DOT_D, DOT_DEPTH)
for (r, a0, a1) in WIFI_ARCS:
    marks = marks.union(ball_groove(WIFI_ARC_C[0], WIFI_ARC_C[1], r, a0, a1))
marks = marks.union(dimple(CENTER_DOT[0], CENTER_DOT[1], CENTER_DOT_D, 0.35))

try:
    txt = None
    for ch, x, y, ang in LETTERS:
        g = (cq.Workplane("XY")
             .text(ch, TXT_SIZE, ENG_H, kind="bold", halign="center", valign="center")
             .rotate((0, 0, 0), (0, 0, 1), ang)
             .translate((x, y, Z_ENG)))
        txt = g if txt is None else txt.union(g)
    marks = marks.union(txt)
except Exception:
    pass  # text is decorative; keep the part valid if no font is available

body = body.cut(marks)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
